import math
import cadquery as cq

# ---------------- Driving dimensions (mm) ----------------
W = 64.0            # block width  (X)
D = 64.0            # block depth  (Y)
H = 32.0            # block height (Z)

hole_x = -16.4      # hole centre X (from block centre)
hole_y = 12.7       # hole centre Y (from block centre)

csk_d = 13.0        # countersink diameter at the top face
csk_angle = 82.0    # countersink included angle (82 deg flat-head)
thread_d = 6.1      # nominal (major) thread diameter where the countersink ends
tap_d = 5.0         # tapped bore at the thread minor diameter (thread shown as a plain bore)
bore_depth = 12.0   # depth of the tapped bore below the top face
tip_angle = 60.0    # included angle of the conical thread run-out at the bottom
bottom_d = 3.8      # flat at the bottom of the hole

seam_angle = 0.0    # angle of the revolved cutter seam (+X: hidden in the main view)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- Block ----------------
block = cq.Workplane("XY").box(W, D, H).translate((0, 0, H / 2.0))

# ---------------- Countersunk tapped blind hole (one revolved cutter) ----------------
csk_depth = (csk_d - thread_d) / 2.0 / math.tan(math.radians(csk_angle / 2.0))
tip_depth = (tap_d - bottom_d) / 2.0 / math.tan(math.radians(tip_angle / 2.0))
over = 1.0  # cutter overshoot above the top face (continues the countersink cone)
k = math.tan(math.radians(csk_angle / 2.0))

# half profile (radius, z) with z measured from the top face, drawn in the XZ plane
profile = [
    (0.0, over),
    (csk_d / 2.0 + over * k, over),
    (thread_d / 2.0, -csk_depth),
    (tap_d / 2.0, -csk_depth),
    (tap_d / 2.0, -bore_depth),
    (bottom_d / 2.0, -bore_depth - tip_depth),
    (0.0, -bore_depth - tip_depth),
]
cutter = (
    cq.Workplane("XZ")
    .polyline(profile).close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), seam_angle)
    .translate((hole_x, hole_y, H))
)

result = block.cut(cutter)
